import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 240.0          # overall length along X
W = 122.0          # width of the Y-shaped head (along Y)
T = 7.0            # plate thickness
ARM_W = 35.0       # width of the straight arm
HEAD_FLAT = 35.0   # X-length of the straight part of the head ears
NOTCH_D = 17.5     # depth of the rectangular notch in the head end
NOTCH_H = 52.0     # height (Y) of that notch
HOLE_D = 7.0       # mounting holes in the ears
HOLE_X = 17.5      # hole centre distance from the head end
HOLE_Y = 43.5      # hole centre offset from centreline
BOSS_L = 41.5      # raised obround pad length
BOSS_W = 17.0      # raised obround pad width
BOSS_H = 3.2       # pad height above plate
BOSS_R = 1.0       # pad top-edge round
SLOT_L = 21.0      # through slot length
SLOT_W = 7.5       # through slot width
BOSS_X = [113.0, 205.0]   # pad / slot centres measured from head end
EDGE_R = 0.6       # small round on all upper edges (plate, holes, pads, slots)
BASE_R = 1.0       # pad root fillet

# ---------------- outline ----------------
x0 = -L / 2.0
diag_end = HEAD_FLAT + (W / 2.0 - ARM_W / 2.0)   # 45 deg shoulder
pts = [
    (0.0, W / 2),
    (HEAD_FLAT, W / 2),
    (diag_end, ARM_W / 2),
    (L, ARM_W / 2),
    (L, -ARM_W / 2),
    (diag_end, -ARM_W / 2),
    (HEAD_FLAT, -W / 2),
    (0.0, -W / 2),
    (0.0, -NOTCH_H / 2),
    (NOTCH_D, -NOTCH_H / 2),
    (NOTCH_D, NOTCH_H / 2),
    (0.0, NOTCH_H / 2),
]
pts = [(x + x0, y) for x, y in pts]

plate = cq.Workplane("XY").polyline(pts).close().extrude(T)

# ear holes
plate = (
    plate.faces(">Z").workplane(origin=(0, 0, T))
    .pushPoints([(x0 + HOLE_X, HOLE_Y), (x0 + HOLE_X, -HOLE_Y)])
    .hole(HOLE_D)
)

# break every upper edge of the plate (outline + hole rims)
plate = plate.faces(">Z").edges().fillet(EDGE_R)

# raised obround pads with rounded top edge
for bx in BOSS_X:
    pad = (
        cq.Workplane("XY", origin=(0, 0, T))
        .center(x0 + bx, 0)
        .slot2D(BOSS_L, BOSS_W)
        .extrude(BOSS_H)
        .faces(">Z").edges()
        .fillet(BOSS_R)
    )
    plate = plate.union(pad)

# small root fillet where each pad meets the plate
for bx in BOSS_X:
    cx = x0 + bx
    plate = plate.edges(
        cq.selectors.BoxSelector(
            (cx - BOSS_L / 2 - 1, -BOSS_W / 2 - 1, T - 0.1),
            (cx + BOSS_L / 2 + 1, BOSS_W / 2 + 1, T + 0.1),
        )
    ).fillet(BASE_R)

# through slots, rims rounded on the pad top
for bx in BOSS_X:
    cx = x0 + bx
    cutter = (
        cq.Workplane("XY", origin=(0, 0, -1))
        .center(cx, 0)
        .slot2D(SLOT_L, SLOT_W)
        .extrude(T + BOSS_H + 2)
    )
    plate = plate.cut(cutter)
    ztop = T + BOSS_H
    plate = plate.edges(
        cq.selectors.BoxSelector(
            (cx - SLOT_L / 2 - 0.5, -SLOT_W / 2 - 0.5, ztop - 0.1),
            (cx + SLOT_L / 2 + 0.5, SLOT_W / 2 + 0.5, ztop + 0.1),
        )
    ).fillet(EDGE_R)

result = plate
